"""Relief model: a rectangular terrain block (flat bottom, four vertical sides) whose
top carries three mountain ranges, an isolated ridge on the front edge and two deep
valleys running out of the right-hand (+X) side.

Every landform is a CAD feature: mountains are lofts through a handful of horizontal
elliptical sections (footprint -> summit), valleys are lofted trough cutters, and the
whole relief is finally trimmed to the block outline.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 102.0      # X extent of the relief block
L = 150.0      # Y extent of the relief block
PLAIN = 14.0   # height of the flat plain (top of base slab)
ZMAX = 30.0    # maximum height of the terrain

# cross-section profiles of the mountain lofts:
#   (height fraction, scale of half-length a, scale of half-width b)
DOME = [(0.0, 1.0, 1.0), (0.3, 0.9, 0.9), (0.65, 0.72, 0.72), (0.88, 0.48, 0.48), (1.0, 0.18, 0.18)]
PEAK = [(0.0, 1.0, 1.0), (0.35, 0.78, 0.78), (0.7, 0.5, 0.5), (0.92, 0.26, 0.26), (1.0, 0.1, 0.1)]
RIDGE = [(0.0, 1.0, 1.0), (0.4, 0.9, 0.62), (0.75, 0.7, 0.32), (1.0, 0.35, 0.1)]
APRON = [(0.0, 1.0, 1.0), (0.4, 0.82, 0.82), (0.75, 0.55, 0.55), (1.0, 0.2, 0.2)]
MASSIF = [(0.0, 1.0, 1.0), (0.3, 0.95, 0.95), (0.6, 0.87, 0.87), (0.85, 0.7, 0.7), (0.96, 0.45, 0.45), (1.0, 0.2, 0.2)]
BAND = [(0.0, 1.0, 1.0), (0.35, 0.95, 0.92), (0.7, 0.85, 0.72), (0.9, 0.72, 0.45), (1.0, 0.55, 0.18)]

# hills: (cx, cy, top_z, a, b, angle_deg, profile, lean_x, lean_y)
#   a = half length along angle, b = half width (a >= b)
#   lean = horizontal shift of the summit relative to the footprint centre
HILLS = [
    # gentle aprons (pediments) at the foot of the ranges
    (26.0, 21.0, 16.5, 24.0, 12.0, 40.0, APRON, -4.0, 9.0),   # in front of chain 1
    (80.0, 76.0, 18.0, 30.0, 16.0, 60.0, APRON, -8.0, 6.0),   # between chain 2 and chain 3
    # left range (chain 1, running SW -> NE)
    (20.5, 34.6, 19.5, 24.0, 9.0, 44.4, BAND, -1.5, 1.5),    # chain 1 band
    (7.5, 23.5, 27.7, 9.0, 6.5, 80.0, DOME, 0.0, 0.0),       # P1/P2 massif
    (35.5, 51.0, 30.0, 8.5, 7.0, 45.0, MASSIF, 0.0, 0.0),    # P3 dome
    (38.0, 31.0, 21.5, 13.0, 9.0, 35.0, DOME, -2.0, 2.0),    # SE spur of chain 1 below P3
    (52.0, 56.5, 20.5, 8.0, 6.0, 60.0, RIDGE, 0.0, 0.0),     # saddle between P3/P4 and P5
    # centre range (chain 2, running W -> E)
    (80.0, 33.0, 22.0, 27.0, 12.0, -12.0, BAND, 0.0, 2.0),   # chain 2 band
    (82.5, 34.0, 25.5, 7.0, 6.0, -12.0, DOME, 0.0, 0.0),     # knob on chain 2
    (67.0, 37.0, 29.6, 12.0, 11.0, -12.0, MASSIF, -3.0, 5.0), # P4 dome (steep SE face)
    (101.0, 31.5, 28.7, 10.5, 10.0, 90.0, DOME, 0.0, 0.0),   # PR
    # right range (chain 3, running SW -> NE)
    (72.0, 83.0, 18.5, 10.0, 6.0, 40.0, RIDGE, 0.0, 0.0),    # low ridge P5 -> P7
    (87.0, 96.0, 28.0, 10.5, 9.0, 90.0, PEAK, 0.0, 0.0),     # P7 cone
    (67.5, 115.5, 29.0, 10.5, 8.0, 50.0, MASSIF, 0.0, 0.0),  # P6 massif
    (83.0, 128.0, 21.0, 11.0, 5.5, 44.0, MASSIF, 0.0, 0.0),  # saddle ridge P6 -> PB
    (98.0, 141.5, 29.5, 12.5, 9.0, 0.0, DOME, 0.0, 0.0),     # PB
]

# front-edge ridge PF, given directly as loft sections (cx, cy, z, a, b, angle)
PF_SECTIONS = [
    (40.0, -1.0, 13.0, 17.0, 6.5, 0.0),
    (45.0, -1.0, 16.5, 10.0, 5.8, 0.0),
    (47.5, -1.0, 19.0, 6.5, 4.0, 0.0),
    (49.0, -1.0, 22.0, 4.0, 2.8, 0.0),
    (50.3, -1.0, 24.4, 1.2, 1.1, 0.0),
]

# P5 massif: summit at its south-west end, long shoulder running north-east
P5_SECTIONS = [
    (61.0, 73.5, 13.0, 12.0, 8.0, 30.0),
    (60.0, 73.0, 18.0, 11.0, 7.5, 30.0),
    (58.5, 72.3, 22.0, 9.0, 6.8, 30.0),
    (56.5, 72.0, 25.5, 6.0, 5.0, 30.0),
    (55.0, 71.8, 28.0, 3.5, 3.2, 30.0),
    (54.5, 71.6, 29.0, 1.5, 1.3, 30.0),
]

# valleys / hollows, each given as loft sections (cx, cy, z, a, b, angle) from the bottom up
VALLEY_A = [  # deep valley at the front-right, floor falling towards the +X edge
    (100.0, 15.5, 4.5, 14.0, 1.5, 0.0),
    (95.0, 14.5, 8.0, 20.0, 4.0, 0.0),
    (88.0, 13.0, 11.0, 26.0, 6.5, 0.0),
    (84.0, 11.0, 13.5, 32.0, 8.5, 0.0),
    (82.0, 10.0, 15.5, 34.0, 10.0, 0.0),
]
VALLEY_B = [  # deep valley at the back-right, running along the right range
    (103.0, 126.0, 2.0, 4.0, 1.5, 49.0),
    (100.0, 122.5, 5.0, 7.0, 3.5, 49.0),
    (97.0, 119.5, 9.0, 11.0, 5.5, 49.0),
    (95.0, 117.5, 12.5, 15.0, 7.5, 49.0),
    (95.0, 117.0, 15.5, 19.0, 9.5, 49.0),
]
TROUGH_R = [  # shallow trough along the right edge
    (104.0, 98.0, 12.2, 11.0, 1.0, 90.0),
    (104.0, 98.0, 13.5, 16.0, 5.0, 90.0),
    (104.0, 98.0, 15.0, 20.0, 8.0, 90.0),
]
HOLLOW_FL = [  # shallow hollow at the front-left corner
    (10.0, -3.0, 11.0, 9.0, 1.0, 0.0),
    (10.0, -3.0, 13.0, 13.0, 5.0, 0.0),
    (10.0, -3.0, 15.0, 16.0, 8.0, 0.0),
]
# (sections, wall section above the trough or None): the wall section is the ellipse
# at the top of the steep ruled wall rising from the trough rim
VALLEYS = [
    (VALLEY_A, (81.0, 9.5, ZMAX + 2.0, 35.0, 11.0, 0.0)),
    (VALLEY_B, (96.3, 116.2, ZMAX + 2.0, 18.0, 9.6, 49.0)),
    (TROUGH_R, None),
    (HOLLOW_FL, None),
]


def ellipse_wire(cx, cy, z, a, b, ang):
    """Horizontal ellipse at height z, half-axes a (along angle ang) and b."""
    d = cq.Vector(math.cos(math.radians(ang)), math.sin(math.radians(ang)), 0)
    if b > a:  # keep the major axis along d so that lofted sections stay aligned
        a = b + 1e-3
    return cq.Wire.assembleEdges(
        [cq.Edge.makeEllipse(a, b, cq.Vector(cx, cy, z), cq.Vector(0, 0, 1), d)]
    )


def loft_sections(sections):
    """Smooth loft through horizontal elliptical sections (bottom to top)."""
    return cq.Solid.makeLoft([ellipse_wire(*s) for s in sections], False)


def hill(cx, cy, top, a, b, ang, prof, lx=0.0, ly=0.0, z0=PLAIN - 1.0):
    """Mountain feature: footprint ellipse sunk 1 mm into the slab, summit at top."""
    h = top - z0
    return loft_sections([(cx + f * lx, cy + f * ly, z0 + f * h, a * sa, b * sb, ang)
                          for f, sa, sb in prof])


def valley(sections, wall):
    """Valley cutter: smooth lofted trough, optionally plus a steep ruled wall above its
    rim, so that mountain flanks bordering the valley are cut back to cliffs."""
    trough = loft_sections(sections)
    if wall is None:
        return trough
    upper = cq.Solid.makeLoft([ellipse_wire(*sections[-1]), ellipse_wire(*wall)], True)
    return trough.fuse(upper).clean()


# base slab
body = cq.Workplane("XY").box(W, L, PLAIN, centered=False)

for p in HILLS:
    body = body.union(cq.Workplane("XY").add(hill(*p)))

for secs in (PF_SECTIONS, P5_SECTIONS):
    body = body.union(cq.Workplane("XY").add(loft_sections(secs)))

for v in VALLEYS:
    body = body.cut(cq.Workplane("XY").add(valley(*v)))

# trim everything to the block footprint
clip = cq.Workplane("XY").box(W, L, ZMAX + 10, centered=False)
result = body.intersect(clip)

VIEW = {"azimuth": 45, "elevation": 26}
